import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Keycap, built in a local frame: local z = keycap height axis (global +Y),
# local x = global X, local y = global -Z.  Opening plane at z = 0.
BASE_W = 18.0          # outer width at the opening (X)
BASE_D = 18.0          # outer depth at the opening (local y)
H = 11.2               # keycap height (opening -> top face)
TOP_W = 12.4           # outer width of the top face (X)
TOP_D = 14.5           # outer depth of the top face
CORNER_R = 1.2         # rounding of the four lateral edges
WALL = 1.2             # wall thickness at the opening
TOP_T = 1.3            # thickness of the top plate
IN_TOP_W = 10.5        # cavity width at the top plate
IN_TOP_D = 12.45       # cavity depth at the top plate
POST_R = 1.4           # quarter-round posts in the cavity corners (at the opening)
CAV_R = 0.4            # small rounding of the cavity corner edges

# Cherry MX style stem
STEM_D = 5.55
STEM_BOTTOM = 1.5      # stem end, measured from the opening plane
CROSS_L = 4.5
CROSS_W = 1.85
CROSS_DEPTH = 4.0
RIB_W = 1.0
RIB_FRONT = 5.5        # ribs run from here up to the top plate

# Tea cup sitting on the top face (hemisphere, centre on the rim plane)
CUP_R = 10.0
CUP_H = 9.15           # from keycap top face to the rim
RECESS_DEPTH = 1.85    # "coffee" level below the rim
RIM_WALL = 1.0
HANDLE_R = 2.55        # torus major radius
HANDLE_T = 0.72       # torus tube radius
HANDLE_X = 9.77        # handle ring centre distance from the cup axis
HANDLE_Z = 5.1         # handle ring centre above the keycap top face

# derived
TOP_SHIFT = BASE_D / 2.0 - TOP_D / 2.0      # one side wall stays straight
in_bw = BASE_W - 2 * WALL
in_bd = BASE_D - 2 * WALL
in_top_z = H - TOP_T
in_top_cy = in_bd / 2.0 - IN_TOP_D / 2.0    # cavity keeps that wall straight too


def rrect(w, d, r):
    return cq.Sketch().rect(w, d).vertices().fillet(r)


# ---------------- keycap outer shell ----------------
outer = (
    cq.Workplane("XY")
    .placeSketch(rrect(BASE_W, BASE_D, CORNER_R),
                 rrect(TOP_W, TOP_D, CORNER_R).moved(cq.Location(cq.Vector(0, TOP_SHIFT, H))))
    .loft()
)

# ---------------- cavity ----------------
cavity = (
    cq.Workplane("XY")
    .placeSketch(rrect(in_bw, in_bd, CAV_R).moved(cq.Location(cq.Vector(0, 0, -0.01))),
                 rrect(IN_TOP_W, IN_TOP_D, CAV_R).moved(cq.Location(cq.Vector(0, in_top_cy, in_top_z))))
    .loft()
)
body = outer.cut(cavity)

# corner posts: quarter-round columns standing in the cavity corners at the
# opening; the tapering walls swallow them further in
posts = (cq.Workplane("XY")
         .rect(in_bw, in_bd, forConstruction=True).vertices()
         .circle(POST_R).extrude(in_top_z))
posts = posts.intersect(cavity)
body = body.union(posts)

# ---------------- stem + ribs ----------------
stem = (cq.Workplane("XY").workplane(offset=STEM_BOTTOM)
        .circle(STEM_D / 2.0).extrude(in_top_z - STEM_BOTTOM + 0.2))
ribs = (cq.Workplane("XY").workplane(offset=RIB_FRONT)
        .rect(BASE_W, RIB_W).extrude(in_top_z - RIB_FRONT + 0.2)
        .union(cq.Workplane("XY").workplane(offset=RIB_FRONT)
               .rect(RIB_W, BASE_D).extrude(in_top_z - RIB_FRONT + 0.2)))
ribs = ribs.intersect(cavity)
cross = (cq.Workplane("XY").workplane(offset=STEM_BOTTOM - 0.1)
         .rect(CROSS_L, CROSS_W).extrude(CROSS_DEPTH + 0.1)
         .union(cq.Workplane("XY").workplane(offset=STEM_BOTTOM - 0.1)
                .rect(CROSS_W, CROSS_L).extrude(CROSS_DEPTH + 0.1)))
body = body.union(stem).union(ribs).cut(cross)

# ---------------- cup ----------------
rim_z = H + CUP_H
# lower hemisphere, seam turned to the back-bottom side where it is hidden
sphere = cq.Workplane("XY").add(
    cq.Solid.makeSphere(CUP_R, cq.Vector(0, 0, 0), angleDegrees1=-90, angleDegrees2=0)
    .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 135)
    .translate(cq.Vector(0, TOP_SHIFT, rim_z)))
clip = (cq.Workplane("XY").workplane(offset=H - 0.2)
        .center(0, TOP_SHIFT).rect(2 * CUP_R + 2, 2 * CUP_R + 2).extrude(CUP_H + 0.2))
cup = sphere.intersect(clip)

# handle: a ring (torus) lying in the plane through the cup axis; the tube
# profile sits on the cup side of the ring so its seams end up hidden
ring_c = cq.Vector(HANDLE_X, TOP_SHIFT, H + HANDLE_Z)
tube = cq.Wire.assembleEdges([
    cq.Edge.makeCircle(HANDLE_T, ring_c - cq.Vector(HANDLE_R, 0, 0), cq.Vector(0, 0, 1))])
handle = cq.Workplane("XY").add(
    cq.Solid.revolve(tube, [], 360, ring_c, ring_c + cq.Vector(0, 1, 0)))
cup = cup.union(handle)

recess = (cq.Workplane("XY").workplane(offset=rim_z - RECESS_DEPTH)
          .center(0, TOP_SHIFT).circle(CUP_R - RIM_WALL).extrude(RECESS_DEPTH + 1))
cup = cup.cut(recess)

part = body.union(cup)

# local z (keycap axis) -> global +Y ; local y -> global -Z
result = part.rotate((0, 0, 0), (1, 0, 0), -90)

VIEW = {"azimuth": 45, "elevation": 26}
